"""Rounded finger-tip like body: a round capsule (cylinder + elliptical dome tip)
trimmed by four long flats (back, pad and two diagonal bevels), closed by a
slightly oblique end face, with every trim edge filleted.  The body axis is
tilted in space (tip toward +X / -Y / +Z)."""
import math
import cadquery as cq
from cadquery.occ_impl.shapes import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm / deg), body-local frame ----------------
# local frame: Z = body axis (cut end -> tip), X = width, Y = thickness (+Y = back)
R_BODY = 14.40        # radius of the round envelope (sets the width)
TIP_LEN = 13.15       # axial semi-axis of the elliptical tip dome
Z_TIP = 28.45         # tip apex position on the axis
Z_CUT = -29.56        # end face position on the axis
CUT_TILT_Y = -4.35    # end face tilt about local Y
CUT_TILT_X = 0.03     # end face tilt about local X

FLAT_BACK = 12.94     # back flat (+Y) distance from axis
FLAT_PAD = 11.70      # pad flat (-Y) distance from axis
BEVEL1_ANG = 47.18    # +X+Y bevel: normal angle from +X toward +Y
BEVEL1_D = 9.55       # +X+Y bevel distance from axis
BEVEL2_ANG = 46.63    # -X-Y bevel (pad side facet): normal angle
BEVEL2_D = 9.87       # -X-Y bevel distance from axis
TILT_BACK = 0.00       # taper of each flat toward the tip (deg)
TILT_PAD = 0.12
TILT_BEVEL1 = 0.77
TILT_BEVEL2 = 1.53

R_FLAT = 6.37         # fillet on all flat / bevel edges
R_CUT_BACK = 5.34     # fillet on the back half of the end face edge
R_CUT_PAD = 8.36      # fillet on the pad half of the end face edge

# placement of the body in the part frame
ROLL = 9.64           # roll about the body axis
ALPHA = 47.26         # tip tilted from +Z toward -Y (about X)
BETA = 10.13          # tip tilted toward +X


def half_space(normal, dist, size=400.0):
    """Box filling the half space normal . p > dist (used as a planar cutter)."""
    n = cq.Vector(*normal).normalized()
    blk = cq.Workplane("XY").box(size, size, size).translate((0, 0, size / 2))
    z = cq.Vector(0, 0, 1)
    axis = z.cross(n)
    ang = math.degrees(math.acos(max(-1.0, min(1.0, z.dot(n)))))
    if axis.Length > 1e-9:
        blk = blk.rotate((0, 0, 0), axis.toTuple(), ang)
    elif n.z < 0:
        blk = blk.rotate((0, 0, 0), (1, 0, 0), 180)
    return blk.translate((n * dist).toTuple())


# ---------------- round capsule: cylinder + elliptical dome ----------------
z_dome = Z_TIP - TIP_LEN
z_start = Z_CUT - 40.0
cylinder = (cq.Workplane("XY").circle(R_BODY).extrude(z_dome - z_start)
            .translate((0, 0, z_start)))
dome = (cq.Workplane("XZ").moveTo(0, 0).lineTo(R_BODY, 0)
        .ellipseArc(R_BODY, TIP_LEN, angle1=0, angle2=90, startAtCurrent=True)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .translate((0, 0, z_dome)))
body = cylinder.union(dome)

# ---------------- long flats / bevels ----------------
b1, b2 = math.radians(BEVEL1_ANG), math.radians(BEVEL2_ANG)


def flat_normal(nx, ny, taper):
    t = math.radians(taper)
    return (nx * math.cos(t), ny * math.cos(t), math.sin(t))


flats = [
    (flat_normal(0, 1, TILT_BACK), FLAT_BACK),
    (flat_normal(0, -1, TILT_PAD), FLAT_PAD),
    (flat_normal(math.cos(b1), math.sin(b1), TILT_BEVEL1), BEVEL1_D),
    (flat_normal(-math.cos(b2), -math.sin(b2), TILT_BEVEL2), BEVEL2_D),
]
for n, d in flats:
    body = body.cut(half_space(n, d))

# ---------------- slightly oblique end face ----------------
tx, ty = math.radians(CUT_TILT_Y), math.radians(CUT_TILT_X)
n_cut = cq.Vector(math.sin(tx), -math.sin(ty) * math.cos(tx),
                  -math.cos(ty) * math.cos(tx))
body = body.cut(half_space(n_cut.toTuple(), n_cut.dot(cq.Vector(0, 0, Z_CUT))))

# ---------------- edge rounding (one fillet operation, per-edge radii) ----------------
solid = body.val()
cut_face = [f for f in solid.Faces()
            if f.geomType() == "PLANE" and f.normalAt().dot(n_cut) > 0.999][0]
cut_edges = cut_face.Edges()
flat_edges = []
for f in solid.Faces():
    if f.geomType() == "PLANE" and not f.isSame(cut_face):
        for e in f.Edges():
            if any(e.isSame(c) for c in cut_edges):
                continue
            if not any(e.isSame(u) for u in flat_edges):
                flat_edges.append(e)

mk = BRepFilletAPI_MakeFillet(solid.wrapped)
for e in flat_edges:
    mk.Add(R_FLAT, e.wrapped)
for e in cut_edges:
    mk.Add(R_CUT_BACK if e.Center().y > 0 else R_CUT_PAD, e.wrapped)
mk.Build()
body = cq.Workplane("XY").add(cq.Shape.cast(mk.Shape()))

# ---------------- place the body ----------------
a = math.radians(ALPHA)
body = body.rotate((0, 0, 0), (0, 0, 1), ROLL)
body = body.rotate((0, 0, 0), (1, 0, 0), ALPHA)
body = body.rotate((0, 0, 0), (0, math.cos(a), math.sin(a)), BETA)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
